import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
RING_A = 45.2          # outer semi-axis of the elliptical frame along X
RING_B = 50.0          # outer semi-axis of the elliptical frame along Y
RING_WALL = 4.1        # radial wall thickness of the frame
RING_H = 6.75          # frame height
PLATE_T = 0.6          # thickness of the cut-out figure plate (flush with frame top)
EAR_BAND = 0.75        # width of the thin ear outline bands
SLOT_W = 0.5           # width of the thin through-slots (line art)
HANG_HOLE_D = 2.8      # hanging hole through the front wall (-Y)
HANG_HOLE_Z = 2.75     # height of the hanging-hole axis above the frame bottom
TAB_W = 1.8            # small tab hanging below the frame under the hole
TAB_DEPTH = 0.55
TAB_DROP = 1.0         # how far the tab hangs below the frame bottom
TAB_OVERLAP = 0.6      # how far it reaches up onto the wall
TAB_PROUD = 0.1        # how far its front face stands proud of the wall

# The figure outline was traced on a pixel grid of the plan view; these three
# numbers map that trace onto the frame (centre pixel and pixels per mm).
TRACE_CX = 130.3
TRACE_CY = 389.8
TRACE_PX_PER_MM = 2.367 * (50.0 / RING_B)


def P(px, py):
    """trace pixel -> model mm (Y up)."""
    return ((px - TRACE_CX) / TRACE_PX_PER_MM, (TRACE_CY - py) / TRACE_PX_PER_MM)


def pts(seq):
    return [P(*q) for q in seq]


# ---------------------------------------------------------------------------
# Figure outline: list of segments (each a spline through the given points);
# consecutive segments share their end points, which become corners.
# ---------------------------------------------------------------------------
# point runs shared by the outline and the ear loops
LEFT_EAR_FRONT = [(93.8, 301.2), (94.2, 312.7), (92.9, 324.2)]
LEFT_EAR_BACK = [(82.3, 384.8), (75.4, 380.0), (69.2, 373.8), (64.6, 367.7), (61.0, 360.5),
                 (58.8, 354.0), (57.7, 345.4), (58.3, 335.8), (61.2, 326.2), (66.9, 320.4),
                 (77.5, 319.4)]
LEFT_EAR_NOTCH = [(77.5, 319.4), (76.5, 315.6), (71.7, 308.8)]
RIGHT_EAR_RIM = [(173.7, 337.7), (174.6, 324.2), (176.8, 315.0), (180.2, 310.0), (184.3, 308.0),
                 (187.4, 309.0), (192.8, 314.8), (197.7, 322.3), (201.5, 331.9), (202.5, 343.5),
                 (201.7, 354.0), (199.2, 362.8), (196.0, 370.5), (192.6, 375.4), (187.8, 377.0),
                 (181.8, 375.6)]
RIGHT_EAR_NOTCH = [(181.8, 375.6), (183.3, 379.6), (184.6, 383.1)]

OUTLINE = [
    # bridge inside the frame wall joining the left ear to the frame
    [(73.5, 297.0), (80.0, 293.0), (86.0, 291.5)],
    # left ear, right side, down to the head
    [(86.0, 291.5), (89.5, 293.8), (92.3, 296.5)] + LEFT_EAR_FRONT
    + [(91.4, 334.0), (91.5, 349.2), (92.3, 360.0), (94.5, 366.5)],
    # head top left
    [(94.5, 366.5), (97.2, 359.2), (102.2, 352.4), (110.0, 344.8), (115.6, 340.4),
     (117.5, 338.0)],
    # hair tuft
    [(117.5, 338.0), (119.0, 340.0), (123.3, 338.8), (127.3, 338.0)],
    # head top right
    [(127.3, 338.0), (128.7, 341.4), (134.6, 341.7), (141.5, 342.7), (148.5, 344.4),
     (154.2, 347.3), (159.5, 351.0), (163.5, 355.5), (166.2, 361.5)],
    # right ear
    [(166.2, 361.5), (169.5, 355.0), (172.7, 349.2)] + RIGHT_EAR_RIM,
    RIGHT_EAR_NOTCH,
    # neck right, back and haunch
    [(184.6, 383.1), (181.7, 386.0), (176.9, 388.4), (172.1, 391.7), (167.3, 395.6),
     (164.4, 399.4), (161.5, 404.2), (159.3, 410.0), (159.2, 414.0), (162.0, 416.8),
     (168.8, 418.5), (175.6, 422.3), (180.4, 430.0), (183.3, 437.7), (185.2, 445.4),
     (186.8, 451.2), (190.6, 453.6), (192.4, 458.0), (191.2, 463.5), (188.0, 467.8),
     (182.3, 470.8), (176.0, 473.2), (171.5, 474.6), (168.9, 477.5), (168.9, 482.5),
     (167.0, 488.5), (162.5, 492.5), (157.0, 494.5)],
    # right foot sole, merged into the frame
    [(157.0, 494.5), (152.0, 499.3), (147.5, 498.2), (144.0, 492.8), (139.6, 491.0),
     (136.6, 489.3), (134.4, 487.6)],
    # toes of the left foot
    [(134.4, 487.6), (130.4, 490.0), (126.9, 491.1), (122.3, 493.4), (120.0, 492.4),
     (119.0, 489.5), (117.1, 487.7), (114.8, 487.1), (109.6, 488.8), (106.7, 490.5),
     (105.3, 487.5), (106.0, 484.2), (103.2, 482.5), (102.0, 479.6), (98.0, 479.0),
     (93.0, 478.6), (89.5, 479.8), (86.7, 480.6), (85.6, 479.4)],
    # left paw
    [(85.6, 479.4), (85.6, 472.3), (84.6, 465.4), (84.0, 460.0), (83.9, 455.8),
     (84.6, 451.0), (85.6, 446.2), (87.5, 443.8), (90.4, 443.3), (93.3, 445.2),
     (95.7, 448.1), (98.1, 448.1), (101.0, 445.7), (103.4, 444.2)],
    # left arm up to the shoulder
    [(103.4, 444.2), (104.3, 440.4), (102.9, 436.5), (101.6, 431.0), (102.3, 426.5),
     (105.0, 422.0), (109.2, 417.7)],
    # cheek up to the bottom of the left ear
    [(109.2, 417.7), (105.8, 414.2), (101.2, 409.6), (96.5, 405.0), (93.1, 399.2),
     (92.2, 395.2), (92.8, 392.2)],
    # left ear, outer side, back up to the frame
    [(92.8, 392.2), (88.9, 389.2)] + LEFT_EAR_BACK,
    LEFT_EAR_NOTCH,
    [(71.7, 308.8), (73.0, 303.0), (73.5, 297.0)],
]

# closed ear loops; the holes are these loops shrunk by the band width
LEFT_EAR_LOOP = [
    [(75.0, 300.4), (81.0, 296.1), (86.5, 293.2)],
    [(86.5, 293.2), (89.5, 293.9), (92.2, 296.6)] + LEFT_EAR_FRONT
    + [(90.9, 332.5), (89.6, 336.5)],
    [(89.6, 336.5), (85.5, 344.5), (82.7, 352.5), (82.4, 360.0), (82.1, 367.7),
     (83.1, 375.0), (84.6, 381.2)],
    # the band widens towards the bottom of the ear
    [(84.6, 381.2), (81.2, 380.6), (76.6, 378.3), (70.4, 374.5), (65.8, 369.1),
     (61.6, 361.0)] + LEFT_EAR_BACK[5:],
    LEFT_EAR_NOTCH,
    [(71.7, 308.8), (73.2, 303.0), (75.0, 300.4)],
]

RIGHT_EAR_LOOP = [
    [(172.9, 385.8), (173.3, 378.0), (173.8, 365.0), (173.5, 350.0)] + RIGHT_EAR_RIM,
    RIGHT_EAR_NOTCH,
    [(184.6, 383.1), (178.5, 385.2), (172.9, 385.8)],
]

# eyes: (cx, cy, a, b, angle of the a-axis in deg) with a pupil disc (cx, cy, r)
# left standing against the rim
EYES = [
    ((108.8, 366.0, 10.0, 8.6, 45.0), (113.5, 359.5, 2.5)),
    ((159.0, 365.0, 9.9, 5.8, -70.0), (161.0, 359.5, 2.0)),
]

# nostrils: round end (cx, cy, r) and tip point
NOSTRILS = [
    ((127.5, 367.8, 2.8), (134.8, 376.3)),
    ((148.3, 367.3, 1.6), (144.0, 375.2)),
]

# mouth: the upper teeth are one crescent-shaped opening divided into teeth by a
# thin zig-zag web; the lower teeth are separate small triangular openings
TEETH_WEB = 0.4
UPPER_MOUTH = [
    [(97.0, 388.6), (104.0, 386.2), (111.2, 384.9), (122.0, 383.0), (129.6, 381.9),
     (133.8, 381.8), (141.8, 381.8), (148.2, 383.5), (156.2, 385.7), (163.2, 388.4)],
    [(163.2, 388.4), (161.5, 393.0), (157.5, 397.0), (153.5, 397.0), (149.0, 393.9),
     (141.8, 390.6), (132.8, 388.6), (122.0, 391.4), (111.2, 395.8), (105.5, 396.2),
     (100.0, 395.0), (97.0, 388.6)],
]
UPPER_TEETH_ZIGZAG = [
    (97.0, 388.6), (101.5, 394.5), (104.0, 386.2), (108.0, 394.8), (111.2, 384.9),
    (117.5, 394.0), (122.0, 383.0), (125.5, 390.8), (129.6, 381.9), (132.0, 385.6),
    (133.8, 381.8), (138.0, 389.8), (141.8, 381.8), (145.0, 390.3), (148.2, 383.5),
    (152.5, 394.0), (156.2, 385.7), (159.5, 394.8), (163.2, 388.4),
]
LOWER_TEETH = [
    [(103.6, 397.0), (103.9, 401.6), (110.6, 399.2)],
    [(104.3, 402.2), (105.4, 406.4), (111.2, 403.0)],
    [(108.0, 405.6), (112.0, 410.6), (116.4, 403.6)],
    [(114.8, 411.2), (121.6, 415.2), (122.0, 406.2)],
    [(125.6, 417.4), (132.3, 417.4), (129.0, 411.6)],
    [(135.6, 417.4), (142.2, 417.4), (139.0, 411.6)],
    [(143.4, 414.0), (150.0, 410.2), (144.2, 405.2)],
    [(150.6, 409.2), (155.0, 405.0), (150.0, 401.6)],
    [(153.8, 403.4), (157.8, 400.2), (153.4, 397.8)],
]

# chest fur patch with its long tail slot running down beside the arm
CHEST = [
    [(114.5, 420.0), (123.5, 421.0), (132.0, 423.5)],
    [(132.0, 423.5), (130.6, 429.5), (129.2, 437.5), (126.8, 447.0), (122.5, 456.0)],
    [(122.5, 456.0), (119.3, 450.2), (116.5, 443.5), (114.3, 439.5)],
    # fur tufts: material spikes pointing into the patch from its left edge
    [(114.3, 439.5), (118.0, 432.0)],
    [(118.0, 432.0), (112.3, 435.5)],
    [(112.3, 435.5), (116.8, 427.5)],
    [(116.8, 427.5), (110.8, 431.0)],
    [(110.8, 431.0), (116.5, 423.3)],
    [(116.5, 423.3), (109.8, 426.5)],
    [(109.8, 426.5), (114.5, 420.0)],
]
SLOTS = [
    # arm / body line continuing the chest patch
    [(122.2, 455.0), (120.8, 460.5), (119.6, 466.0), (120.0, 472.0)],
    # paw / arm line
    [(103.6, 444.6), (101.0, 452.0), (100.6, 459.0), (101.8, 466.0)],
    # gaps between the claws of the paw and the toes (open at the outline)
    [(83.8, 475.8), (89.5, 475.0), (94.0, 473.8)],
    [(103.6, 484.6), (107.5, 482.6), (111.5, 480.2)],
    [(104.6, 489.0), (109.5, 486.8), (114.0, 484.8)],
    [(118.2, 491.8), (124.5, 489.8), (129.5, 488.0)],
]

# shallow engraved lines on the top face (haunch, leg and paw outlines)
GROOVE_W = 0.35
GROOVE_D = 0.25
GROOVES = [
    [(94.0, 473.8), (98.5, 472.0), (103.0, 470.3)],
    [(153.8, 438.5), (154.6, 447.0), (156.2, 454.5)],
    [(142.7, 461.9), (147.5, 457.0), (153.0, 454.3), (160.0, 453.5), (165.5, 455.2),
     (170.5, 459.0)],
    [(134.6, 481.0), (133.6, 474.0), (134.6, 467.5), (138.5, 464.6), (143.0, 463.5),
     (147.3, 462.5), (153.1, 460.6), (157.9, 461.4), (161.7, 466.3), (164.6, 471.2),
     (166.6, 475.5)],
]

# round through-holes (cx, cy, rx, ry): paw pads and toe pads
PADS = [
    (150.6, 481.8, 9.1, 9.6),     # big sole pad of the right foot
    (137.9, 469.2, 2.0, 2.3),
    (154.0, 464.3, 2.9, 2.1),
    (165.0, 481.3, 1.6, 2.7),
    (88.6, 445.9, 2.3, 2.1),      # left paw pads
    (87.2, 459.1, 2.2, 2.7),
]


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def wire_from_segments(segments):
    """Closed wire of spline segments (2-point segments become lines)."""
    edges = []
    for seg in segments:
        p = [cq.Vector(x, y, 0) for x, y in pts(seg)]
        if len(p) == 2:
            edges.append(cq.Edge.makeLine(p[0], p[1]))
        else:
            edges.append(cq.Edge.makeSpline(p))
    return cq.Wire.assembleEdges(edges)


def poly_wire(seq):
    p = [cq.Vector(x, y, 0) for x, y in pts(seq)]
    return cq.Wire.makePolygon(p, close=True)


def prism(wire, t, z0):
    f = cq.Face.makeFromWires(wire)
    if f.normalAt().z < 0:
        f = cq.Face(f.wrapped.Reversed())
    s = cq.Solid.extrudeLinear(f, cq.Vector(0, 0, t)).translate(cq.Vector(0, 0, z0))
    if not s.isValid():
        s = s.fix()
    return s


def respline(wire):
    """Re-express offset edges as plain interpolating splines (clean STEP)."""
    edges = []
    for e in wire.Edges():
        if e.geomType() in ("LINE", "CIRCLE"):
            edges.append(e)
            continue
        n = max(4, min(14, int(e.Length() / 0.6) + 2))
        p = [e.positionAt(i / (n - 1)) for i in range(n)]
        edges.append(cq.Edge.makeSpline(p))
    return cq.Wire.assembleEdges(edges)


def ellipse_wire(cx, cy, rx, ry, ang=0.0):
    x, y = P(cx, cy)
    rx, ry = rx / TRACE_PX_PER_MM, ry / TRACE_PX_PER_MM
    if abs(rx - ry) < 1e-6:
        e = cq.Edge.makeCircle(rx, pnt=cq.Vector(x, y, 0))
        return cq.Wire.assembleEdges([e])
    if rx < ry:
        rx, ry, ang = ry, rx, ang + 90.0
    a = math.radians(ang)
    e = cq.Edge.makeEllipse(rx, ry, pnt=cq.Vector(x, y, 0),
                            xdir=cq.Vector(math.cos(a), math.sin(a), 0))
    return cq.Wire.assembleEdges([e])


# ---------------------------------------------------------------------------
# frame
# ---------------------------------------------------------------------------
frame = (
    cq.Workplane("XY")
    .ellipse(RING_A, RING_B)
    .ellipse(RING_A - RING_WALL, RING_B - RING_WALL)
    .extrude(RING_H)
)

# hanging hole through the front wall and the little tab under it
hole = (
    cq.Workplane("XZ", origin=(0, -RING_B + RING_WALL / 2, HANG_HOLE_Z))
    .circle(HANG_HOLE_D / 2)
    .extrude(RING_WALL * 2, both=True)
)
frame = frame.cut(hole)
tab = (
    cq.Workplane("XY")
    .box(TAB_W, TAB_DEPTH, TAB_DROP + TAB_OVERLAP, centered=(True, False, False))
    .translate((0, -RING_B - TAB_PROUD, -TAB_DROP))
)
frame = frame.union(tab)

# ---------------------------------------------------------------------------
# figure plate
# ---------------------------------------------------------------------------
z0 = RING_H - PLATE_T
cut_h = PLATE_T + 2.0
cz = z0 - 1.0

plate = prism(wire_from_segments(OUTLINE), PLATE_T, z0)

cutters = []
for loop in (LEFT_EAR_LOOP, RIGHT_EAR_LOOP):
    w = wire_from_segments(loop)
    for iw in w.offset2D(-EAR_BAND, "arc"):
        cutters.append(prism(respline(iw), cut_h, cz))

for (ex, ey, ea, eb, eang), (px_, py_, pr) in EYES:
    eye = prism(ellipse_wire(ex, ey, ea, eb, eang), cut_h, cz)
    pupil = prism(ellipse_wire(px_, py_, pr, pr), cut_h + 1.0, cz - 0.5)
    cutters.append(eye.cut(pupil))

for (cx_, cy_, r), tip in NOSTRILS:
    # teardrop: circle + tangent lines to the tip
    c = cq.Vector(*P(cx_, cy_), 0)
    t = cq.Vector(*P(*tip), 0)
    rr = r / TRACE_PX_PER_MM
    d = (t - c)
    L = d.Length
    u = d.normalized()
    ang = math.acos(rr / L)
    base = math.atan2(u.y, u.x)
    a1, a2 = base + ang, base - ang
    p1 = c + cq.Vector(rr * math.cos(a1), rr * math.sin(a1), 0)
    p2 = c + cq.Vector(rr * math.cos(a2), rr * math.sin(a2), 0)
    pm = c - u * rr
    w = cq.Wire.assembleEdges([
        cq.Edge.makeLine(t, p1),
        cq.Edge.makeThreePointArc(p1, pm, p2),
        cq.Edge.makeLine(p2, t),
    ])
    cutters.append(prism(w, cut_h, cz))

mouth = prism(wire_from_segments(UPPER_MOUTH), cut_h, cz)
zz = cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts(UPPER_TEETH_ZIGZAG)])
for ww in zz.offset2D(TEETH_WEB / 2, "arc"):
    mouth = mouth.cut(prism(ww, cut_h + 1.0, cz - 0.5))
cutters.append(mouth)
for tri in LOWER_TEETH:
    cutters.append(prism(poly_wire(tri), cut_h, cz))

cutters.append(prism(wire_from_segments(CHEST), cut_h, cz))

for s in SLOTS:
    p = [cq.Vector(x, y, 0) for x, y in pts(s)]
    w = cq.Wire.assembleEdges([cq.Edge.makeSpline(p)])
    for ow in w.offset2D(SLOT_W / 2, "arc"):
        cutters.append(prism(respline(ow), cut_h, cz))

for cx_, cy_, rx, ry in PADS:
    cutters.append(prism(ellipse_wire(cx_, cy_, rx, ry), cut_h, cz))

for g in GROOVES:
    p = [cq.Vector(x, y, 0) for x, y in pts(g)]
    w = cq.Wire.assembleEdges([cq.Edge.makeSpline(p)])
    for ow in w.offset2D(GROOVE_W / 2, "arc"):
        cutters.append(prism(respline(ow), 2.0, RING_H - GROOVE_D))

cut_all = cutters[0].fuse(*cutters[1:]).clean()
plate_shape = plate.cut(cut_all)

result = frame.union(cq.Workplane("XY").add(plate_shape)).clean()

VIEW = {"azimuth": 45, "elevation": 26}
